import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 30.0          # overall width  (X)
L = 54.0          # overall length (Y)
H = 9.8           # overall thickness (Z)
C = 8.4           # 45 deg corner chamfer leg (plan view)
S = 1.8           # top rabbet width along the straight sides and ends
T = 2.35          # top rabbet depth
PITCH = 30.0      # centre distance of the two holes (along Y)
CB_D = 13.2       # counterbore diameter
CB_DEPTH = 4.8    # counterbore depth
HOLE_D = 7.7      # through-hole diameter
SEAM_ANG = 45.0   # angular position of the hole cylinders' seam (cosmetic only)

# ---------------- octagonal base plate ----------------
outline = [
    (-W / 2 + C, -L / 2), (W / 2 - C, -L / 2),
    (W / 2, -L / 2 + C), (W / 2, L / 2 - C),
    (W / 2 - C, L / 2), (-W / 2 + C, L / 2),
    (-W / 2, L / 2 - C), (-W / 2, -L / 2 + C),
]
plate = cq.Workplane("XY").polyline(outline).close().extrude(H)

# ---------------- top rabbet ----------------
# A step of width S and depth T is milled along the two long sides and the
# two ends; the 45 deg corner faces run straight through to the top face.
rabbet_cutter = (
    cq.Workplane("XY")
    .workplane(offset=H - T)
    .rect(W + 2 * (S + 5), L + 2 * (S + 5))
    .rect(W - 2 * S, L - 2 * S)
    .extrude(T + 1)
)
plate = plate.cut(rabbet_cutter)

# ---------------- counterbored through holes ----------------
hole_pts = [(0.0, -PITCH / 2), (0.0, PITCH / 2)]
cutters = None
for (xc, yc) in hole_pts:
    thru = (
        cq.Workplane("XY")
        .transformed(offset=(xc, yc, -1.0), rotate=(0, 0, SEAM_ANG))
        .circle(HOLE_D / 2)
        .extrude(H + 2.0)
    )
    cbore = (
        cq.Workplane("XY")
        .transformed(offset=(xc, yc, H - CB_DEPTH), rotate=(0, 0, SEAM_ANG))
        .circle(CB_D / 2)
        .extrude(CB_DEPTH + 1.0)
    )
    c = thru.union(cbore)
    cutters = c if cutters is None else cutters.union(c)

plate = plate.cut(cutters)

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
